import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.Geom import Geom_Ellipse, Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve
from OCP.gp import gp_Ax2, gp_Dir, gp_Pnt

# Hand-held body with a stadium-section tube at the bottom (two blind bores),
# a barrel-shaped grip, a framed recessed window on the front (-Y) and a
# tilted nozzle with a flared neck on top (leaning toward +X).

# ---------------- driving dimensions (mm) ----------------
TUBE_A, TUBE_B = 25.0, 15.3      # stadium tube: half length (X), half width (Y)
TUBE_TOP = 40.0                  # straight tube height (loft starts here)
CAP_A, CAP_B = 24.5, 16.0        # top cap stadium
CAP_TOP = 194.0                  # flat top of the cap
CAP_FILLET = 3.5
CAP_H = 3.7                      # straight cap above the loft (its top edge is rounded)

SECTION_PTS = 24                 # points used to build each smooth section curve

# body loft sections: (half X, half Y back, half Y front, front corner radius, z)
# back half is a stadium end, front half a rounded rectangle (slightly fuller)
BODY_SECTIONS = [
    (TUBE_A, TUBE_B, TUBE_B, TUBE_B - 0.5, TUBE_TOP),
    (TUBE_A, TUBE_B, TUBE_B, TUBE_B - 0.5, 47.0),
    (26.2, 20.3, 21.5, 18.0, 60.0),
    (28.4, 24.6, 25.2, 20.0, 75.0),
    (31.0, 27.0, 26.5, 21.0, 118.0),
    (30.0, 24.4, 25.0, 19.0, 157.0),
    (26.5, 20.3, 21.0, 16.0, 170.0),
    (24.5, 16.2, 16.8, 14.0, 181.0),
    (CAP_A, CAP_B, CAP_B, CAP_B, CAP_TOP - CAP_H),
]

# front frame (pad) and pocket
FRONT_Y = -25.0                  # front face of the frame
PAD_BACK_Y = -5.0
PAD_EDGE_R = 9.0                 # rounding of the frame face toward the sides
PAD_TOP, PAD_BOT = 163.5, 62.5
PAD_TOP_HW, PAD_BOT_HW = 18.0, 20.0
PAD_SIDE_HW = 27.3               # half width of the frame at mid height
PAD_CORNER = 6.5                 # height of the clipped corners
PAD_CORNER_HW_TOP, PAD_CORNER_HW_BOT = 21.5, 22.5   # half width where the side arcs start
POCKET_TOP, POCKET_BOT = 157.0, 69.0
POCKET_TOP_HW, POCKET_BOT_HW = 14.0, 16.0
POCKET_MID_HW = 25.2
MID_Z = 113.0
POCKET_MAX_DEPTH = 16.0
# pocket floor: convex surface lofted through (half X, front depth, corner radius, z);
# shallow at the ends of the window, deeper in the middle and toward the sides
POCKET_FLOOR = [
    (25.0, 22.0, 12.0, 60.0),
    (27.5, 19.5, 12.0, 88.0),
    (28.0, 17.0, 12.0, 118.0),
    (27.5, 19.0, 12.0, 145.0),
    (24.0, 22.5, 12.0, 170.0),
]
POCKET_CORNER_R = 3.0

# nozzle
NOZ_BASE_X = 4.2                 # where the nozzle axis meets the cap top plane
NOZ_TILT = 25.5                  # degrees from vertical toward +X
NOZ_LEN = 43.2                   # from cap top to tip along axis
NOZ_D = 17.0                     # tip tube
NOZ_D_LOW = 17.6                 # top of the flared neck (small step to the tip tube)
NOZ_STEP_H = 21.2                # axial height of the step above the cap top
NOZ_BORE = 6.0
# flared neck: horizontal elliptic sections (z, x_min, x_max, half width y)
NECK_SECTIONS = [
    (191.5, -6.5, 23.0, 12.8),
    (197.0, -2.4, 19.8, 10.8),
    (204.0, 0.75, 20.5, 9.8),
]

# small hole in the top
TOP_HOLE_X = -8.0
TOP_HOLE_D = 6.0
TOP_HOLE_DEPTH = 4.0

# two bores at the bottom
BOT_HOLE_D = 20.0
BOT_HOLE_X = 11.0
BOT_HOLE_DEPTH = 9.0


def section_wire(a, bb, bf, rc, z, exact=False):
    """Closed body section at height z as ONE smooth periodic spline edge:
    back half = stadium end of radius bb, front half = rounded rectangle
    (depth bf, corner radius rc)."""
    c45 = math.cos(math.pi / 4)
    sb = a - bb
    sf = a - rc
    hf = bf - rc
    w = (
        cq.Workplane("XY")
        .workplane(offset=z)
        .moveTo(0, bb)
        .lineTo(-sb, bb)
        .threePointArc((-sb - bb * c45, bb * c45), (-a, 0))
    )
    if hf > 1e-6:
        w = w.lineTo(-a, -hf)
    w = (
        w.threePointArc((-sf - rc * c45, -hf - rc * c45), (-sf, -bf))
        .lineTo(sf, -bf)
        .threePointArc((sf + rc * c45, -hf - rc * c45), (a, -hf))
    )
    if hf > 1e-6:
        w = w.lineTo(a, 0)
    w = (
        w.threePointArc((sb + bb * c45, bb * c45), (sb, bb))
        .close()
        .wire()
        .val()
    )
    if exact:
        # exact outline merged into one B-spline edge (matches analytic solids exactly)
        # chain the edges starting at the back point (0, bb) so the start matches the smooth sections
        edges = w.Edges()
        cur = cq.Vector(0, bb, z)
        conv = GeomConvert_CompCurveToBSplineCurve()
        for _ in range(len(edges)):
            for e in edges:
                if (e.startPoint() - cur).Length < 1e-6:
                    f, l = BRep_Tool.Range_s(e.wrapped)
                    conv.Add(Geom_TrimmedCurve(BRep_Tool.Curve_s(e.wrapped, f, l), f, l), 1e-6, True)
                    cur = e.endPoint()
                    break
        return cq.Wire.assembleEdges([cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge())])
    # resample into one smooth (C2) periodic spline -> single face, smooth shading
    pts = [w.positionAt(k / SECTION_PTS) for k in range(SECTION_PTS)]
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True)])


def loft(wires):
    b = BRepOffsetAPI_ThruSections(True, False, 1e-6)
    b.SetSmoothing(False)
    b.SetMaxDegree(3)
    for w in wires:
        b.AddWire(w.wrapped)
    b.Build()
    return cq.Solid(b.Shape())


# ---------------- main body ----------------
tube_face = cq.Face.makeFromWires(section_wire(*BODY_SECTIONS[0][:4], 0.0))
tube = cq.Solid.extrudeLinear(tube_face, cq.Vector(0, 0, TUBE_TOP))
bulge = loft([section_wire(*s) for s in BODY_SECTIONS[:-1]] + [section_wire(*BODY_SECTIONS[-1], exact=True)])
# cap: the top section extruded straight up, its top edge rounded
cap_wire = section_wire(*BODY_SECTIONS[-1], exact=True)
cap_solid = cq.Solid.extrudeLinear(cq.Face.makeFromWires(cap_wire), cq.Vector(0, 0, CAP_H))
cap = cq.Workplane("XY").add(cap_solid).faces(">Z").edges().fillet(CAP_FILLET)
body = cq.Workplane("XY").add(tube).union(cq.Workplane("XY").add(bulge)).union(cap)


# ---------------- nozzle ----------------
def ellipse_wire(center, r1, r2, normal, d1):
    """closed ellipse (r1 along d1, r2 across) as one B-spline edge starting at +d1"""
    c = gp_Pnt(center.x, center.y, center.z)
    n = gp_Dir(normal.x, normal.y, normal.z)
    if r1 >= r2:
        g = Geom_Ellipse(gp_Ax2(c, n, gp_Dir(d1.x, d1.y, d1.z)), r1, r2)
        u0 = 0.0
    else:
        d2 = normal.cross(d1)
        g = Geom_Ellipse(gp_Ax2(c, n, gp_Dir(d2.x, d2.y, d2.z)), r2, r1)
        u0 = -math.pi / 2
    bs = GeomConvert.CurveToBSplineCurve_s(Geom_TrimmedCurve(g, u0, u0 + 2 * math.pi))
    return cq.Wire.assembleEdges([cq.Edge(BRepBuilderAPI_MakeEdge(bs).Edge())])


t = math.radians(NOZ_TILT)
axis = cq.Vector(math.sin(t), 0, math.cos(t))
xdir_t = cq.Vector(math.cos(t), 0, -math.sin(t))
base = cq.Vector(NOZ_BASE_X, 0, CAP_TOP)
tip = base + axis * NOZ_LEN
step_pt = base + axis * NOZ_STEP_H

# (all neck sections start at the back, +Y, so the loft seam is out of the main view)
neck_wires = [
    ellipse_wire(cq.Vector((x0 + x1) / 2, 0, z), hy, (x1 - x0) / 2, cq.Vector(0, 0, 1), cq.Vector(0, 1, 0))
    for (z, x0, x1, hy) in NECK_SECTIONS
]
neck_wires.append(ellipse_wire(step_pt, NOZ_D_LOW / 2, NOZ_D_LOW / 2, axis, cq.Vector(0, 1, 0)))
neck = loft(neck_wires)
noz_up = cq.Solid.makeCylinder(NOZ_D / 2, NOZ_LEN - NOZ_STEP_H, step_pt, axis)
body = body.union(cq.Workplane("XY").add(neck)).union(cq.Workplane("XY").add(noz_up))

# small hole in the cap top
body = body.cut(
    cq.Workplane("XY")
    .workplane(offset=CAP_TOP - TOP_HOLE_DEPTH)
    .center(TOP_HOLE_X, 0)
    .circle(TOP_HOLE_D / 2)
    .extrude(TOP_HOLE_DEPTH + 2)
)

# ---------------- front frame pad ----------------
def octagon(y0, depth):
    """frame outline in the XZ plane at y=y0, extruded toward +Y by depth"""
    return (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .moveTo(-PAD_TOP_HW, PAD_TOP)
        .lineTo(PAD_TOP_HW, PAD_TOP)
        .lineTo(PAD_CORNER_HW_TOP, PAD_TOP - PAD_CORNER)
        .threePointArc((PAD_SIDE_HW, MID_Z), (PAD_CORNER_HW_BOT, PAD_BOT + PAD_CORNER))
        .lineTo(PAD_BOT_HW, PAD_BOT)
        .lineTo(-PAD_BOT_HW, PAD_BOT)
        .lineTo(-PAD_CORNER_HW_BOT, PAD_BOT + PAD_CORNER)
        .threePointArc((-PAD_SIDE_HW, MID_Z), (-PAD_CORNER_HW_TOP, PAD_TOP - PAD_CORNER))
        .close()
        .extrude(-depth)  # XZ normal is -Y -> negative extrude goes to +Y
    )


pad_full = octagon(FRONT_Y - 15.0, PAD_BACK_Y - FRONT_Y + 15.0)
# front surface: flat in the middle, rounding back toward the sides
front_env = (
    cq.Workplane("XY")
    .center(0, FRONT_Y + 30.0)
    .rect(2 * (PAD_SIDE_HW + 0.5), 60.0)
    .extrude(400)
    .translate((0, 0, -100))
    .edges("|Z and <Y")
    .fillet(PAD_EDGE_R)
)
pad = pad_full.intersect(front_env)
waste = pad_full.cut(front_env)
body = body.cut(waste).union(pad)

# ---------------- pocket with curved floor ----------------
pocket_prism = (
    cq.Workplane("XZ", origin=(0, FRONT_Y - 10.0, 0))
    .moveTo(-POCKET_TOP_HW, POCKET_TOP)
    .lineTo(POCKET_TOP_HW, POCKET_TOP)
    .threePointArc((POCKET_MID_HW, MID_Z), (POCKET_BOT_HW, POCKET_BOT))
    .lineTo(-POCKET_BOT_HW, POCKET_BOT)
    .threePointArc((-POCKET_MID_HW, MID_Z), (-POCKET_TOP_HW, POCKET_TOP))
    .close()
    .extrude(-(10.0 + POCKET_MAX_DEPTH))
)
try:
    pocket_prism = pocket_prism.edges("|Y").fillet(POCKET_CORNER_R)
except Exception:
    pass
# the pocket floor is the front of a convex inner loft
inner = loft([section_wire(a, 14.0, bf, rc, z) for (a, bf, rc, z) in POCKET_FLOOR])
pocket = pocket_prism.cut(cq.Workplane("XY").add(inner))
body = body.cut(pocket)

# ---------------- holes ----------------
# bore at the nozzle tip
bore = cq.Solid.makeCylinder(NOZ_BORE / 2, 25.0, tip - axis * 24.0, axis)
body = body.cut(cq.Workplane("XY").add(bore))

# two bores in the bottom
body = body.cut(
    cq.Workplane("XY")
    .pushPoints([(-BOT_HOLE_X, 0), (BOT_HOLE_X, 0)])
    .circle(BOT_HOLE_D / 2)
    .extrude(BOT_HOLE_DEPTH)
)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
